import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
OR_OUT = 88.4        # outer ring, outer radius
OR_IN = 79.2         # outer ring, inner radius
IR_OUT = 47.8        # inner ring, outer radius
IR_IN = 38.4         # inner ring, inner radius
RING_H = 2.8         # ring height
CH_DEPTH = 1.7       # depth of the LED channel in the top of the rings
LIP = 1.0            # lip width either side of the channel
SLOT_LEN = 9.4       # wire slots through the channel floor
IN_SLOT_LEN = 10.8

DIGIT_T = 4.2        # extrusion height of the numerals
HOUR_H = (OR_IN - IR_OUT) + 0.4   # cap height of hour numerals (spans the gap)
HOUR_R = 0.5 * (OR_IN + IR_OUT)   # radius of hour numeral centres
LABEL_H = 30.0                    # cap height of outer minute labels
LABEL_R = OR_OUT + 0.5 * LABEL_H - 0.6

# font metrics (in units of cap height)
STROKE = 0.105
ADV = 0.76          # advance of a numeral
ADV_ONE = 0.48      # the "1" is a narrow (proportional) numeral
ONE_STEM = 0.30     # left edge of the "1" stem in glyph coordinates
ONE_OFF = 0.03      # stem centre sits this far right of the glyph centre
HOUR_REF_R = 78.0   # radius on which hour-numeral spacing is measured
LABEL_REF_R = 103.0
# per-number (shift, extra letter spacing) in mm along the reading direction
STR_ADJ = {"12": (2.7, 3.7), "L15": (2.4, -2.6)}

# electronics box under 12 o'clock
BOX_W = 32.8
BOX_Y0 = 11.0
BOX_D = 17.7
BOX_WALL = 1.2
BOX_TOP = 2.0
PORT_W = 14.0
PORT_Z0 = 3.1
PORT_Z1 = 15.4
BACK_HOLE_D = 4.6
BACK_HOLE_Z = 12.3
TOP_HOLE_D = 5.4
TOP_HOLE_XY = (-BOX_W / 2 + 5.3, BOX_Y0 + 5.5)

# ---------------------------------------------------------------------------
# stroke font helpers (unit cap height)
# ---------------------------------------------------------------------------
V = cq.Vector


def _up(face):
    """make sure a planar face has its normal along +Z."""
    if face.normalAt().z < 0:
        face = cq.Face(face.wrapped.Reversed())
    return face


def _poly_face(pts):
    w = cq.Wire.makePolygon([V(x, y, 0) for x, y in pts], close=True)
    return _up(cq.Face.makeFromWires(w))


def _rect(x0, y0, x1, y1):
    return _poly_face([(x0, y0), (x1, y0), (x1, y1), (x0, y1)])


def _line(p0, p1, w=STROKE):
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    nx, ny = -dy / L * w / 2, dx / L * w / 2
    return _poly_face([(p0[0] + nx, p0[1] + ny), (p1[0] + nx, p1[1] + ny),
                       (p1[0] - nx, p1[1] - ny), (p0[0] - nx, p0[1] - ny)])


def _ell_edge(cx, cy, rx, ry, a0=None, a1=None):
    if a0 is None:
        if abs(rx - ry) < 1e-9:
            return cq.Edge.makeCircle(rx, V(cx, cy, 0))
        return cq.Edge.makeEllipse(rx, ry, V(cx, cy, 0))
    if abs(rx - ry) < 1e-9:
        return cq.Edge.makeCircle(rx, V(cx, cy, 0), V(0, 0, 1), a0, a1)
    return cq.Edge.makeEllipse(rx, ry, V(cx, cy, 0), V(0, 0, 1), V(1, 0, 0), a0, a1)


def _ring(cx, cy, rxo, ryo, rxi, ryi):
    wo = cq.Wire.assembleEdges([_ell_edge(cx, cy, rxo, ryo)])
    wi = cq.Wire.assembleEdges([_ell_edge(cx, cy, rxi, ryi)])
    return _up(cq.Face.makeFromWires(wo, [wi]))


def _arc(cx, cy, rx, ry, t0, t1, w=STROKE):
    """elliptical arc stroke between parametric angles t0..t1 (deg, t0<t1)."""
    a, b = min(t0, t1), max(t0, t1)
    h = w / 2
    eo = _ell_edge(cx, cy, rx + h, ry + h, a, b)
    ei = _ell_edge(cx, cy, rx - h, ry - h, a, b)
    l1 = cq.Edge.makeLine(eo.endPoint(), ei.endPoint())
    l2 = cq.Edge.makeLine(ei.startPoint(), eo.startPoint())
    wire = cq.Wire.assembleEdges([eo, l1, ei, l2])
    return _up(cq.Face.makeFromWires(wire))


def _ell_pt(cx, cy, rx, ry, t):
    r = math.radians(t)
    return (cx + rx * math.cos(r), cy + ry * math.sin(r))


def _rot180(prims, cx, cy):
    out = []
    for p in prims:
        out.append(p.rotate(V(cx, cy, 0), V(cx, cy, 1), 180))
    return out


def _glyph_prims(ch):
    s = STROKE
    h = s / 2
    if ch == "0":
        return [_ring(0.375, 0.5, 0.335, 0.5, 0.335 - 0.115, 0.5 - 0.095)], (0.03, 0.72)
    if ch == "1":
        x0, x1 = ONE_STEM, ONE_STEM + 0.11
        stem = _rect(x0, 0.0, x1, 1.0)
        A = (x0 + 0.02, 1.0)
        B = (x0 - 0.27, 0.70)
        ux, uy = B[0] - A[0], B[1] - A[1]
        L = math.hypot(ux, uy)
        ux, uy = ux / L, uy / L
        C = (B[0] - uy * s * 0.95, B[1] + ux * s * 0.95)
        # back along -u to the stem left edge
        t = (x0 + 0.03 - C[0]) / (-ux)
        D = (C[0] - ux * t, C[1] - uy * t)
        flag = _poly_face([A, B, C, D])
        return [stem, flag], (0.0, x1 + 0.01)
    if ch == "2":
        # bowl + reverse-curvature (S) stroke down to the base bar
        cx, cy, rx, ry = 0.375, 0.705, 0.275, 1.0 - h - 0.705
        te = -68.0
        bowl = _arc(cx, cy, rx, ry, te, 165.0)
        p = _ell_pt(cx, cy, rx, ry, te)
        r = math.radians(te)
        dx, dy = rx * math.sin(r), -ry * math.cos(r)
        dl = math.hypot(dx, dy)
        dx, dy = dx / dl, dy / dl
        nx, ny = -dy, dx                      # left of travel direction
        q = (0.045, 0.075)
        pqx, pqy = p[0] - q[0], p[1] - q[1]
        rr = -(pqx * pqx + pqy * pqy) / (2.0 * (nx * pqx + ny * pqy))
        ccx, ccy = p[0] + nx * rr, p[1] + ny * rr
        a0 = math.degrees(math.atan2(p[1] - ccy, p[0] - ccx))
        a1 = math.degrees(math.atan2(q[1] - ccy, q[0] - ccx))
        while a1 < a0:
            a1 += 360.0
        sweep = _arc(ccx, ccy, rr, rr, a0, a1)
        bar = _rect(0.03, 0.0, 0.72, s)
        return [bowl, sweep, bar], (0.03, 0.72)
    if ch == "3":
        ym = 0.55
        ryt = (1.0 - h - ym) / 2
        ryb = (ym - h) / 2
        top = _arc(0.37, ym + ryt, 0.25, ryt, -90.0, 160.0)
        bot = _arc(0.39, h + ryb, 0.2775, ryb, -155.0, 90.0)
        mid = _line((0.27, ym), (0.40, ym))
        return [top, bot, mid], (0.03, 0.72)
    if ch == "4":
        xs0, xs1 = 0.47, 0.58
        yb0, yb1 = 0.235, 0.235 + s
        stem = _rect(xs0, 0.0, xs1, 1.0)
        bar = _rect(0.01, yb0, 0.72, yb1)
        x1 = 0.45
        for _ in range(20):
            beta = math.atan2(1.0 - yb1, x1 - 0.01)
            wdt = s / math.sin(beta)
            x1 = xs1 - wdt
        diag = _poly_face([(x1, 1.0), (xs1, 1.0), (0.01 + wdt, yb1), (0.01, yb1)])
        return [stem, bar, diag], (0.01, 0.72)
    if ch == "5":
        bar = _rect(0.15, 1.0 - s, 0.63, 1.0)
        stem = _line((0.205, 1.05), (0.145, 0.47))
        r = 0.275
        bowl = _arc(0.39, h + r, r, r, -142.0, 150.0)
        return [bar, stem, bowl], (0.04, 0.72)
    if ch in "69":
        cx, cy, rx, ry = 0.3775, 0.33, 0.2825, 0.33 - h
        bowl = _ring(cx, cy, rx + h, ry + h, rx - h, ry - h)
        up = _arc(cx, cy, rx, 1.0 - h - cy, 42.0, 180.0)
        prims = [bowl, up]
        if ch == "9":
            prims = _rot180(prims, 0.3775, 0.5)
        return prims, (0.035, 0.72)
    if ch == "7":
        bar = _rect(0.04, 1.0 - s, 0.72, 1.0)
        diag = _line((0.672, 0.97), (0.25, -0.1), s * 1.05)
        return [bar, diag], (0.04, 0.72)
    if ch == "8":
        ym = 0.56
        ryt = (1.0 - h - ym) / 2
        ryb = (ym - h) / 2
        top = _ring(0.3775, ym + ryt, 0.245 + h, ryt + h, 0.245 - h, ryt - h)
        bot = _ring(0.3775, h + ryb, 0.29 + h, ryb + h, 0.29 - h, ryb - h)
        return [top, bot], (0.035, 0.72)
    raise ValueError(ch)


_GLYPH_CACHE = {}


def glyph_face(ch):
    """planar face(s) of one numeral, cap height 1."""
    if ch not in _GLYPH_CACHE:
        prims, (bx0, bx1) = _glyph_prims(ch)
        f = prims[0]
        for p in prims[1:]:
            f = f.fuse(p)
        f = f.intersect(_rect(bx0, 0.0, bx1, 1.0)).clean()
        _GLYPH_CACHE[ch] = f
    return _GLYPH_CACHE[ch]


def _adv(ch):
    return ADV_ONE if ch == "1" else ADV


def _glyph_cx(ch):
    """reference (centre) x of a glyph inside its own coordinates."""
    if ch == "1":
        return ONE_STEM + 0.055 - ONE_OFF
    return 0.375


def arc_numeral(text, cap_h, r_c, r_ref, theta0, thick, shift=0.0, track=0.0):
    """numeral string set on a circular path: every glyph is turned so that its
    'up' points radially outward.  Glyph centres sit on radius r_c, spacing is
    measured as arc length on radius r_ref, string centred on angle theta0."""
    centres = []
    acc = 0.0
    for i, ch in enumerate(text):
        centres.append(acc + _adv(ch) / 2.0 + i * track / cap_h)
        acc += _adv(ch)
    mid = 0.5 * (centres[0] + centres[-1])
    out = []
    for ch, c in zip(text, centres):
        s = (c - mid) * cap_h + shift
        th = theta0 - math.degrees(s / r_ref)
        sols = []
        for face in glyph_face(ch).Faces():
            sol = cq.Solid.extrudeLinear(face, V(0, 0, thick / cap_h))
            sols.append(sol.translate(V(-_glyph_cx(ch), -0.5, 0)))
        g = cq.Compound.makeCompound(sols).scale(cap_h)
        g = g.rotate(V(0, 0, 0), V(0, 0, 1), th - 90.0)
        r = math.radians(th)
        out.append(g.translate(V(r_c * math.cos(r), r_c * math.sin(r), 0)))
    return out


# ---------------------------------------------------------------------------
# rings with LED channel
# ---------------------------------------------------------------------------
def channel_ring(r_in, r_out):
    body = (cq.Workplane("XY").circle(r_out).circle(r_in).extrude(RING_H))
    chan = (cq.Workplane("XY").workplane(offset=RING_H - CH_DEPTH)
            .circle(r_out - LIP).circle(r_in + LIP).extrude(CH_DEPTH + 1.0))
    return body.cut(chan)


outer_ring = channel_ring(OR_IN, OR_OUT)
inner_ring = channel_ring(IR_IN, IR_OUT)
base = outer_ring.union(inner_ring)

# ---------------------------------------------------------------------------
# electronics box hanging under 12 o'clock (open at the bottom)
# ---------------------------------------------------------------------------
# the far end of the box is cylindrical, flush with the outer ring's rim
box_len = OR_OUT + 2.0 - BOX_Y0
box = (cq.Workplane("XY")
       .box(BOX_W, box_len, BOX_D, centered=(True, False, False))
       .translate((0, BOX_Y0, -BOX_D)))
box = box.intersect(cq.Workplane("XY").workplane(offset=-BOX_D - 1.0)
                    .circle(OR_OUT).extrude(BOX_D + 2.0))
cavity = (cq.Workplane("XY")
          .box(BOX_W - 2 * BOX_WALL, box_len, BOX_D - BOX_TOP + 1.0,
               centered=(True, False, False))
          .translate((0, BOX_Y0 + BOX_WALL, -BOX_D - 1.0)))
cavity = cavity.intersect(cq.Workplane("XY").workplane(offset=-BOX_D - 2.0)
                          .circle(OR_OUT - BOX_WALL).extrude(BOX_D + 4.0))
box = box.cut(cavity)
# USB / access port in the front wall
port = (cq.Workplane("XZ").center(0, -0.5 * (PORT_Z0 + PORT_Z1))
        .rect(PORT_W, PORT_Z1 - PORT_Z0).extrude(-BOX_WALL - 2.0)
        .translate((0, BOX_Y0 - 1.0, 0)))
box = box.cut(port)
# cable hole in the back wall
back_hole = (cq.Workplane("XZ").center(0, -BACK_HOLE_Z).circle(BACK_HOLE_D / 2)
             .extrude(-BOX_WALL - 4.0).translate((0, OR_OUT - BOX_WALL - 2.0, 0)))
box = box.cut(back_hole)
# screw hole in the top
top_hole = (cq.Workplane("XY").center(*TOP_HOLE_XY).circle(TOP_HOLE_D / 2)
            .extrude(BOX_TOP + 2.0).translate((0, 0, -BOX_TOP - 1.0)))
box = box.cut(top_hole)

base = base.union(box)

# ---------------------------------------------------------------------------
# wire slots through the channel floor (and the box top below them)
# ---------------------------------------------------------------------------
slot_depth = RING_H + 1.0
slots = None
for k in range(4):
    ang = 90.0 * k
    sl = (cq.Workplane("XY")
          .center(0.5 * (OR_IN + OR_OUT), 0.5 * SLOT_LEN)
          .rect(OR_OUT - OR_IN - 2 * LIP, SLOT_LEN)
          .extrude(slot_depth + BOX_TOP)
          .translate((0, 0, -BOX_TOP - 0.5))
          .rotate((0, 0, 0), (0, 0, 1), ang))
    slots = sl if slots is None else slots.union(sl)
in_slot = (cq.Workplane("XY")
           .center(0, 0.5 * (IR_IN + IR_OUT))
           .rect(IN_SLOT_LEN, IR_OUT - IR_IN - 2 * LIP)
           .extrude(slot_depth + BOX_TOP)
           .translate((0, 0, -BOX_TOP - 0.5)))
slots = slots.union(in_slot)
base = base.cut(slots)

# ---------------------------------------------------------------------------
# numerals
# ---------------------------------------------------------------------------
num_shapes = []
for hr in range(1, 13):
    txt = str(hr)
    sh, tr = STR_ADJ.get(txt, (0.0, 0.0))
    num_shapes += arc_numeral(txt, HOUR_H, HOUR_R, HOUR_REF_R, 90.0 - 30.0 * hr,
                              DIGIT_T, sh, tr)
for txt, phi in (("0", 90.0), ("15", 0.0), ("30", -90.0), ("45", 180.0)):
    sh, tr = STR_ADJ.get("L" + txt, (0.0, 0.0))
    num_shapes += arc_numeral(txt, LABEL_H, LABEL_R, LABEL_REF_R, phi,
                              DIGIT_T, sh, tr)

# one multi-argument boolean for all numerals (kept un-"cleaned": merging the
# coplanar faces here trips up the face unifier)
base = cq.Workplane("XY").add(base.val().fuse(*num_shapes))

result = base
